import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FL_LEN = 237.6        # stadium flange overall length (X)
FL_DEP = 58.6         # stadium flange depth (Y)
FL_T = 10.3           # flange thickness
FL_FIL = 9.0          # rounded top edge of flange
HOLE_D = 7.8          # flange mounting holes
HOLE_XL = -65.8       # left hole X (holes are not symmetric)
HOLE_XR = 52.6        # right hole X

BLK_W = 71.0          # block width (X)
BLK_H = 40.0          # block height below top surface
BLK_GAP = 6.4         # block front face behind flange rear edge
BLK_R = 5.5           # concave radius flange-underside -> block front
BLK_LEN = 65.9        # block rear face behind flange rear edge

WALL_T = 2.5          # side wall (tab) thickness
WALL_EXT = 20.9       # side wall extension past block rear face
TAB_H = 8.2           # tab height above top surface

BORE_D = 19.0         # cross bore through the block
BORE_Y = 28.6         # bore centre behind flange rear edge
BORE_Z = -19.0        # bore centre height

BOSS_R = 5.4          # D-shaped detent bosses on inner faces of wall tabs
BOSS_H = 2.6          # protrusion of the bosses
BOSS_CH = 2.9         # Y-run of the lead-in chamfer on the rear side of each boss
BOSS_Z = (2.6, -31.9) # boss centre heights
BOSS_YOFF = 77.5      # boss centre behind flange rear edge

# ---------------- derived ----------------
YC = 0.0                          # stadium centre in Y
Y_FR = YC + FL_DEP / 2.0          # flange rear edge
Y_W = Y_FR + BLK_GAP              # block front face
Y_R = Y_FR + BLK_LEN              # block rear face
Y_E = Y_R + WALL_EXT              # end of side walls
BOSS_Y = Y_FR + BOSS_YOFF

# ---------------- flange ----------------
flange = (
    cq.Workplane("XY")
    .workplane(offset=-FL_T)
    .slot2D(FL_LEN, FL_DEP, 0)
    .extrude(FL_T)
)
flange = flange.faces(">Z").edges().fillet(FL_FIL)

# ---------------- block (side profile in YZ, extruded along X) ----------------
y0 = Y_FR - FL_FIL - 0.6
prof = (
    cq.Workplane("YZ", origin=(-BLK_W / 2.0, 0, 0))
    .moveTo(y0, 0)
    .lineTo(Y_R, 0)
    .lineTo(Y_R, -BLK_H)
    .lineTo(Y_W, -BLK_H)
    .lineTo(Y_W, -FL_T - BLK_R)
    .radiusArc((Y_W - BLK_R, -FL_T), -BLK_R)
    .lineTo(y0, -FL_T)
    .close()
    .extrude(BLK_W)
)

body = flange.union(prof)

# ---------------- side walls extending past the block ----------------
for sx in (-1, 1):
    x_out = sx * BLK_W / 2.0
    wall = cq.Workplane("XY").box(
        WALL_T, Y_E - Y_R + 0.01, BLK_H + TAB_H, centered=False
    ).translate((x_out - (WALL_T if sx > 0 else 0), Y_R - 0.01, -BLK_H))
    body = body.union(wall)
    # D-shaped detent bosses on the inner face
    x_in = x_out - sx * WALL_T
    for bz in BOSS_Z:
        cyl = cq.Solid.makeCylinder(
            BOSS_R, BOSS_H + 0.2,
            cq.Vector(x_in + sx * 0.2, BOSS_Y, bz),
            cq.Vector(-sx, 0, 0),
        )
        # top-view profile: rear side chamfered (lead-in) from the wall face
        xt = x_in - sx * BOSS_H
        keep = (
            cq.Workplane("XY", origin=(0, 0, bz - BOSS_R - 1))
            .polyline([
                (x_in + sx * 0.5, BOSS_Y - BOSS_R - 1),
                (x_in + sx * 0.5, BOSS_Y + BOSS_R + 0.5),
                (x_in, BOSS_Y + BOSS_R),
                (xt, BOSS_Y + BOSS_R - BOSS_CH),
                (xt, BOSS_Y - BOSS_R - 1),
            ]).close()
            .extrude(2 * BOSS_R + 2)
        )
        boss = cq.Workplane("XY").add(cyl).intersect(keep)
        body = body.union(boss)

# ---------------- holes ----------------
mount_holes = (
    cq.Workplane("XY", origin=(0, 0, 1.0))
    .pushPoints([(HOLE_XL, YC), (HOLE_XR, YC)])
    .circle(HOLE_D / 2.0)
    .extrude(-(FL_T + 2.0))
)
body = body.cut(mount_holes)
bore = cq.Solid.makeCylinder(
    BORE_D / 2.0, BLK_W + 20,
    cq.Vector(-BLK_W / 2.0 - 10, Y_FR + BORE_Y, BORE_Z),
    cq.Vector(1, 0, 0),
)
body = body.cut(cq.Workplane("XY").add(bore))

result = body.clean()

VIEW = {"azimuth": 45, "elevation": 26}
